import math
import cadquery as cq

# ---------------- driving dimensions (mm) : #10-24 x 5/8" pan head Phillips screw
# screw axis = Y ; head underside at y = 0 ; crown toward -Y ; shank toward +Y
D_MAJOR = 4.75        # thread major diameter
D_MINOR = 3.46        # thread root diameter
PITCH = 1.070         # thread pitch (~24 TPI at this scale)
L_SHANK = 16.17       # length under head
THREAD_ROOT_IN = 0.06 # tooth base sits this far inside the root cylinder
SEG_TURNS = 5         # thread turns per swept segment
THREAD_SHIFT = 0.394  # axial phase of the thread (mm)
TIP_D = 3.45          # diameter of the flat end face of the shank
TIP_ANGLE = 45.0      # end chamfer angle (deg from axis)

HEAD_D = 9.37         # head diameter
HEAD_H = 3.37         # total head height (underside to crown apex)
DOME_R = 7.63         # crown (dome) sphere radius
CROWN_R = 1.04        # rounding between crown and side
HEAD_UNDER_R = 0.55   # rounding at the underside rim

# Phillips recess
REC_R = 2.6           # radius of the arm tips at the crown surface
REC_W = 1.38          # arm width at the crown
REC_SIDE_TAPER = 9.0  # taper of the arm side walls (deg)
REC_END_ANGLE = 26.5  # arm end walls (cone half angle, deg from axis)
REC_END_DEPTH = 1.35  # axial depth of the arm end walls
REC_DEPTH = 2.65      # depth of the recess point below the crown apex
REC_WEB = 1.5         # distance of the diagonal webs from the axis at the crown
REC_WEB_TAPER = 9.0   # taper of the web faces (deg)
REC_ROT = 8.0         # rotation of the cross about the axis (deg, CCW seen from the crown)

SEAM_ROT = -(REC_ROT + 270.0)  # park the revolve seams along the lower recess arm (least visible)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- head : one smooth spline profile revolved about Y
# The ideal pan-head profile (underside round, straight side, crown round, spherical dome)
# is sampled with exact tangents and re-interpolated as ONE spline, giving a single smooth face.
R = HEAD_D / 2.0
H = HEAD_H
ru = HEAD_UNDER_R
yd = -H + DOME_R                      # dome centre on the axis
# crown round (radius rc) tangent to the side r = R and to the dome (internally)
rc = CROWN_R
yc = yd - math.sqrt((DOME_R - rc) ** 2 - (R - rc) ** 2)   # centre height of the crown round
a_c = math.atan2(yc - yd, R - rc)     # direction dome-centre -> round-centre (angle in r,y)

def arc_pts(cx, cy, rad, a0, a1, n):
    out = []
    for i in range(n + 1):
        a = a0 + (a1 - a0) * i / n
        p = (cx + rad * math.cos(a), cy + rad * math.sin(a))
        s = 1.0 if a1 > a0 else -1.0
        t = (-math.sin(a) * s, math.cos(a) * s)
        out.append((p, t))
    return out

prof = []
prof += arc_pts(R - ru, -ru, ru, math.pi / 2, 0.0, 3)                 # underside round
prof += [((R, (-ru + yc) / 2.0), (0.0, -1.0))]                           # middle of the side
prof += arc_pts(R - rc, yc, rc, 0.0, a_c, 5)                              # crown round
a_end = -math.pi / 2
dome = arc_pts(0.0, yd, DOME_R, a_c, a_end, 5)
prof += dome[1:]                                                          # spherical dome
spl_pts = [p for p, t in prof]
spl_tan = [t for p, t in prof]

head = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(*spl_pts[0])
    .spline(spl_pts[1:], tangents=spl_tan, includeCurrent=True, scale=False)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# ---------------- shank (built along +Z, turned onto +Y afterwards)
r_maj = D_MAJOR / 2.0
r_min = D_MINOR / 2.0
r_tip = TIP_D / 2.0
c_len = (r_maj + 0.3 - r_tip) / math.tan(math.radians(TIP_ANGLE))
Y0 = -0.3                                   # shank starts a little inside the head

# envelope of the shank: plain cylinder with the end chamfer down to the flat end face
trim = cq.Solid.revolve(
    cq.Face.makeFromWires(cq.Wire.makePolygon([
        cq.Vector(0, 0, Y0),
        cq.Vector(r_maj + 0.3, 0, Y0),
        cq.Vector(r_maj + 0.3, 0, L_SHANK - c_len),
        cq.Vector(r_tip, 0, L_SHANK),
        cq.Vector(0, 0, L_SHANK),
    ], close=True)),
    360.0, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1),
)


def helical_shank():
    # right hand V thread: a triangular tooth swept along a helix.  The sweep is made for a few
    # turns only and repeated end to end (whole turns, so the copies join exactly), which keeps
    # the boolean operations robust; the copies are fused to the root cylinder.
    r_b = r_min - THREAD_ROOT_IN            # tooth base, just inside the root cylinder
    hw_b = PITCH / 2.0 - 0.005              # base half width (< pitch/2 : turns never overlap)
    helix = cq.Wire.makeHelix(PITCH, SEG_TURNS * PITCH, r_b)
    tooth = cq.Wire.makePolygon([
        cq.Vector(r_b, 0, -hw_b), cq.Vector(r_maj, 0, 0), cq.Vector(r_b, 0, hw_b)], close=True)
    seg = cq.Solid.sweep(tooth, [], helix, isFrenet=True)
    z0 = Y0 - PITCH + THREAD_SHIFT
    nseg = int(math.ceil((L_SHANK + PITCH - z0) / (SEG_TURNS * PITCH)))
    segs = [seg.translate(cq.Vector(0, 0, z0 + k * SEG_TURNS * PITCH)) for k in range(nseg)]
    thread = segs[0].fuse(*segs[1:], glue=True)
    core = cq.Solid.makeCylinder(r_min, L_SHANK - Y0 + 1.0, cq.Vector(0, 0, Y0 - 0.5))
    sh = core.fuse(thread).intersect(trim)
    solids = sh.Solids()
    if len(solids) != 1 or not sh.isValid():
        raise ValueError("helical thread failed")
    return solids[0]


def ring_shank():
    # fallback: annular V rings (plain revolved geometry)
    pts = [cq.Vector(0, 0, Y0 - 0.2), cq.Vector(r_maj, 0, Y0 - 0.2)]
    z = 0.05
    pts.append(cq.Vector(r_maj, 0, z))
    while z < L_SHANK + PITCH:
        pts.append(cq.Vector(r_min, 0, z + PITCH / 2.0))
        pts.append(cq.Vector(r_maj, 0, z + PITCH))
        z += PITCH
    pts.append(cq.Vector(0, 0, z))
    rings = cq.Solid.revolve(cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True)),
                             360.0, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    return rings.intersect(trim)


try:
    shank_solid = helical_shank()
except Exception:
    shank_solid = ring_shank()

# +Z -> +Y (rotation keeps the thread right handed)
shank = cq.Workplane("XY").add(shank_solid).rotate((0, 0, 0), (1, 0, 0), -90)

screw = head.union(shank).rotate((0, 0, 0), (0, 1, 0), SEAM_ROT)

# ---------------- Phillips recess tool
# local frame: recess axis +Z, crown apex at z = 0, recess goes toward -Z.
UP = 1.5                         # tool extends above the crown
t_end = math.tan(math.radians(REC_END_ANGLE))

def crown_z(r):
    # crown (dome) height at radius r relative to the apex (negative = below)
    return -(DOME_R - math.sqrt(DOME_R ** 2 - r ** 2))

z_tip = crown_z(REC_R)                      # crown level at the arm tips
r_end_bot = REC_R - REC_END_DEPTH * t_end   # radius at the foot of the end walls
z_end_bot = z_tip - REC_END_DEPTH
# envelope: end-wall cone + conical floor down to the point.
# (revolve seam parked on a web diagonal so that most of it is trimmed away)
env = (
    cq.Workplane("XZ")
    .polyline([
        (0, UP),
        (REC_R + (UP - z_tip) * t_end, UP),
        (r_end_bot, z_end_bot),
        (0, -REC_DEPTH),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), 45)
)

# cross of tapered arms + diamond webs
t_side = math.tan(math.radians(REC_SIDE_TAPER))
hw_top = REC_W / 2.0 + UP * t_side
hw_bot = max(0.1, REC_W / 2.0 - REC_DEPTH * t_side)
L = REC_R + 2.0

def arm(angle_deg):
    a = (
        cq.Workplane("YZ")
        .polyline([(-hw_bot, -REC_DEPTH - 0.2), (hw_bot, -REC_DEPTH - 0.2), (hw_top, UP), (-hw_top, UP)])
        .close()
        .extrude(L, both=True)
    )
    return a.rotate((0, 0, 0), (0, 0, 1), angle_deg)

# webs between the arms: flat faces on the diagonals (a tapered square turned 45 deg)
t_web = math.tan(math.radians(REC_WEB_TAPER))
s_top = (REC_WEB + UP * t_web) * 2.0
s_bot = max(0.1, (REC_WEB - (REC_DEPTH + 0.2) * t_web)) * 2.0
web = (
    cq.Workplane("XY").workplane(offset=-REC_DEPTH - 0.2)
    .rect(s_bot, s_bot)
    .workplane(offset=REC_DEPTH + 0.2 + UP)
    .rect(s_top, s_top)
    .loft()
    .rotate((0, 0, 0), (0, 0, 1), 45)
)
cross = arm(0).union(arm(90)).union(web)
tool = cross.intersect(env)
tool = tool.rotate((0, 0, 0), (0, 0, 1), REC_ROT)
# map local +Z -> -Y (out of the crown) : rotate +90 deg about X, move to the apex
tool = tool.rotate((0, 0, 0), (1, 0, 0), 90).translate((0, -H, 0))

result = screw.cut(tool)
